import cadquery as cq
import math

# =====================================================================
#  Round snap-in end cap: flange disc with a hollow plug on its back
#  (top wall with a large blend, side walls, snap hook, channel floor
#   with cove/groove, tray tongue, deep side wall) and through features.
#  Orientation: flange front face at Y=0 facing -Y, plug towards +Y.
#  Layout dimensions are kept in "design units" (flange radius = 118.5)
#  and scaled to millimetres by S.
# =====================================================================

# ---------------- driving dimensions ----------------
D = 60.0                  # flange disc diameter (mm)
R = D / 2.0
S = R / 118.5             # mm per design unit (flange radius = 118.5 units)
T_U = 16.0                # flange thickness (units)
Y_BOX = 47.6              # depth of the main plug box (units, from the front face)
Y_DEEP = 79.0             # depth of the deep side wall / tray tongue

TW_Z0, TW_Z1 = 87.5, 94.1           # top wall bottom / back-edge top
TW_X0, TW_X1 = 0.3, 58.0            # top wall extent in X
TW_ARC_C = (40.7, 117.8)            # (Y, Z) centre of the top blend arc
TW_ARC_R = 24.7                     # radius of the top blend arc

XW_IN, XW_OUT = 70.5, 79.0          # +X wall inner / outer face
HOOK_X = 88.7                       # snap hook outer face
XW_TOP_FRONT, XW_TOP_BACK = 86.45, 77.25
HOOK_Z0 = -23.5                     # underside of hook and +X wall

FLOOR_Z0, FLOOR_Z1 = -16.5, -10.75  # channel floor / tray
COVE_C = (56.1, 6.15)               # (X, Z) centre of cove between floor and +X wall
COVE_R = 16.9

WC_X0, WC_X1 = -99.0, -85.0         # deep -X side wall
WC_Z0, WC_Z1 = -58.25, 61.1
WC_SIDE_BLEND = 20.0
WC_TOP_BLEND = 18.0

HOLE_R = 4.0
HOLE_DEPTH = 12.0                   # blind locating holes in the flange


def u(v):
    return v * S


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(u(x1 - x0), u(y1 - y0), u(z1 - z0), centered=False)
            .translate((u(x0), u(y0), u(z0))))


def yz_prism(pts, x0, x1):
    """closed (Y,Z) profile extruded along +X from x0 to x1"""
    wp = cq.Workplane("YZ", origin=(u(x0), 0, 0))
    return wp.polyline([(u(a), u(b)) for a, b in pts]).close().extrude(u(x1 - x0))


def fillet_yz(y0, z0, r, x0, x1):
    """concave blend between the flange back (Y=y0) and a top face Z=z0, along X"""
    c = (y0 + r, z0 + r)
    m = (c[0] - r * math.sqrt(0.5), c[1] - r * math.sqrt(0.5))
    wp = cq.Workplane("YZ", origin=(u(x0), 0, 0))
    prof = (wp.moveTo(u(y0), u(z0)).lineTo(u(y0 + r), u(z0))
              .threePointArc((u(m[0]), u(m[1])), (u(y0), u(z0 + r))).close())
    return prof.extrude(u(x1 - x0))


def fillet_xy(y0, x0, r, z0, z1, xdir=-1):
    """concave blend between the flange back (Y=y0) and a side face X=x0, along Z"""
    c = (x0 + xdir * r, y0 + r)
    m = (c[0] - xdir * r * math.sqrt(0.5), c[1] - r * math.sqrt(0.5))
    wp = cq.Workplane("XY", origin=(0, 0, u(z0)))
    prof = (wp.moveTo(u(x0), u(y0)).lineTo(u(x0), u(y0 + r))
              .threePointArc((u(m[0]), u(m[1])), (u(x0 + xdir * r), u(y0))).close())
    return prof.extrude(u(z1 - z0))


# ---------------- flange disc ----------------
disc = cq.Workplane("XZ").circle(R).extrude(-u(T_U))

parts = []

# ---- top wall: one concave arc from the flange edge down to the back edge ----
_a0 = math.atan2(TW_Z1 - TW_ARC_C[1], Y_BOX - TW_ARC_C[0])
_a1 = math.radians(-176.0)
_am = (_a0 + _a1) / 2.0
_pt = lambda a: (TW_ARC_C[0] + TW_ARC_R * math.cos(a), TW_ARC_C[1] + TW_ARC_R * math.sin(a))
_p0, _pm, _p1 = _pt(_a0), _pt(_am), _pt(_a1)
top_wall = (cq.Workplane("YZ", origin=(u(TW_X0), 0, 0))
            .moveTo(u(T_U - 1), u(TW_Z0)).lineTo(u(_p0[0]), u(TW_Z0)).lineTo(u(_p0[0]), u(_p0[1]))
            .threePointArc((u(_pm[0]), u(_pm[1])), (u(_p1[0]), u(_p1[1])))
            .lineTo(u(_p1[0]), u(R / S + 5)).lineTo(u(T_U - 1), u(R / S + 5))
            .close().extrude(u(TW_X1 - TW_X0)))
parts.append(top_wall)

# ---- -X side wall of the box: boss foot, mid wall, upper wall, overhanging ledge ----
parts.append(box(-14.2, 8, T_U, Y_BOX, -86.5, -49.5))
parts.append(box(-2.5, 8, T_U, Y_BOX, -86.5, 61))
parts.append(box(0.3, 8, T_U, Y_BOX, 61, 92.5))
parts.append(box(-13.9, 0.3, T_U, Y_BOX, 55, 61))
parts.append(fillet_yz(T_U, 61, 16, -13.9, 0.3))

# ---- +X side wall (sloped top) and snap hook with lead-in ramp ----
parts.append(yz_prism([(T_U, HOOK_Z0), (Y_BOX, HOOK_Z0), (Y_BOX, XW_TOP_BACK), (T_U, XW_TOP_FRONT)],
                      XW_IN, XW_OUT))
parts.append(yz_prism([(T_U, HOOK_Z0), (Y_BOX, HOOK_Z0), (Y_BOX, -9.75), (T_U, 9.75)],
                      XW_OUT, HOOK_X))

# ---- channel floor with a cove blending into the +X wall ----
parts.append(box(8, XW_IN, T_U, Y_BOX, FLOOR_Z0, FLOOR_Z1))
_zd = COVE_C[1] - math.sqrt(COVE_R ** 2 - (XW_IN - COVE_C[0]) ** 2)
_ad = math.atan2(_zd - COVE_C[1], XW_IN - COVE_C[0])
_am2 = (_ad + (-math.pi / 2)) / 2
cove = (cq.Workplane("XZ", origin=(0, u(T_U), 0))
        .moveTo(u(COVE_C[0]), u(COVE_C[1] - COVE_R)).lineTo(u(XW_IN), u(COVE_C[1] - COVE_R))
        .lineTo(u(XW_IN), u(_zd))
        .threePointArc((u(COVE_C[0] + COVE_R * math.cos(_am2)), u(COVE_C[1] + COVE_R * math.sin(_am2))),
                       (u(COVE_C[0]), u(COVE_C[1] - COVE_R)))
        .close().extrude(-u(Y_BOX - T_U)))
parts.append(cove)

# ---- bottom wall with lead-in chamfer underneath ----
parts.append(yz_prism([(T_U, -115), (T_U, -79.5), (Y_BOX, -79.5), (Y_BOX, -86.5)], -14.2, 38))

# ---- tray tongue behind the box ----
parts.append(box(9.4, 35, Y_BOX - 1, Y_DEEP, FLOOR_Z0, FLOOR_Z1))
parts.append(box(9.4, 14.6, Y_BOX - 1, Y_DEEP, FLOOR_Z0, 14.4))
parts.append(box(31, 35, Y_BOX - 1, Y_DEEP, FLOOR_Z0, -2))

# ---- deep -X side wall with blends to the flange ----
parts.append(box(WC_X0, WC_X1, T_U, Y_DEEP, WC_Z0, WC_Z1))
parts.append(fillet_xy(T_U, WC_X0, WC_SIDE_BLEND, WC_Z0 + 6, WC_Z1, xdir=-1))
parts.append(fillet_yz(T_U, WC_Z1, WC_TOP_BLEND, WC_X0 - WC_SIDE_BLEND, WC_X1))

plug = parts[0]
for p in parts[1:]:
    plug = plug.union(p)

# trim the plug to the flange cylinder (blends run out at the flange edge)
env = cq.Workplane("XZ").circle(R).extrude(-u(Y_DEEP + 1))
plug = plug.intersect(env)

body = disc.union(plug)

# ---------------- cut features ----------------
FULL = Y_DEEP + 4


def cut_xz(pts, depth=FULL):
    return (cq.Workplane("XZ", origin=(0, u(-1), 0))
            .polyline([(u(a), u(b)) for a, b in pts]).close().extrude(-u(depth)))


# snap groove along the inner face of the +X wall (continuation of the cove circle)
groove = (cq.Workplane("XZ", origin=(0, u(T_U), 0)).center(u(COVE_C[0]), u(COVE_C[1]))
          .circle(u(COVE_R)).extrude(-u(Y_BOX - T_U + 1))
          .intersect(box(XW_IN, XW_IN + 5, T_U, Y_BOX + 1, -20, 30)))

# upper-left pocket (chamfered corner), lower-left window, hook release slot, horizontal slot
pocket = cut_xz([(-50.05, 97.35), (-27.45, 97.35), (-29.25, 54.55), (-61.95, 54.55), (-60.15, 88.25)])
window = cut_xz([(-70.35, -58.75), (-36.85, -58.75), (-36.85, -87.55), (-70.35, -87.55)])
rslot = cut_xz([(77.8, -23.9), (88.2, -23.9), (88.2, -65.5), (77.8, -65.5)])
slot = (cq.Workplane("XZ", origin=(0, u(-1), 0)).center(u(40.5), u(-1.5))
        .slot2D(u(51), u(7.6), 0).extrude(-u(FULL)))
# two blind locating holes
holes = (cq.Workplane("XZ", origin=(0, u(-1), 0))
         .pushPoints([(u(-91), u(-36.75)), (u(-13.75), u(-54.55))])
         .circle(u(HOLE_R)).extrude(-u(HOLE_DEPTH + 1)))

body = body.cut(groove).cut(pocket).cut(window).cut(rslot).cut(slot).cut(holes)

# shallow ledge recess above the window and tapered spike mark (front face)
ledge = cut_xz([(-73.35, -51.75), (-36.85, -51.75), (-36.85, -58.75), (-73.35, -58.75)], depth=5)
spike = cut_xz([(-61.75, -51.0), (-56.5, -25.0), (-51.5, -51.0)], depth=4)
body = body.cut(ledge).cut(spike)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
